import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 80.0            # plate width (square)
T = 10.0            # plate thickness
R_CORNER = 16.5     # plan-view corner radius
CH_TOP = 1.7        # 45 deg chamfer on top perimeter edge

HOLE_SPACING = 46.8 # centre-to-centre of the 4 holes (square pattern)
HOLE_D = 10.1       # through-hole diameter
CSK_D = 13.1        # countersink outer diameter (top face)
CSK_ANGLE = 90.0    # countersink included angle

REC_D = 27.0        # bottom central recess diameter (at ceiling)
REC_DEPTH = 3.3     # recess depth
REC_CH = 1.3        # 45 deg chamfer on recess mouth

# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(W, W)
    .extrude(T)
    .edges("|Z").fillet(R_CORNER)
)
plate = plate.faces(">Z").edges().chamfer(CH_TOP)

# ---------------- countersunk through holes (from top) ----------------
h = HOLE_SPACING / 2.0
pts = [(-h, -h), (h, -h), (h, h), (-h, h)]
plate = (
    plate.faces(">Z").workplane(origin=(0, 0, T))
    .pushPoints(pts)
    .cskHole(HOLE_D, CSK_D, CSK_ANGLE)
)

# ---------------- bottom central recess with chamfered mouth ----------------
r = REC_D / 2.0
recess = (
    cq.Workplane("XZ")
    .polyline([
        (0.0, -1.0),
        (r + REC_CH + 1.0, -1.0),
        (r + REC_CH + 1.0, 0.0),
        (r + REC_CH, 0.0),
        (r, REC_CH),
        (r, REC_DEPTH),
        (0.0, REC_DEPTH),
    ]).close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)
plate = plate.cut(recess)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
